"""Square lid / cover plate on four corner standoffs ("SD-CARD USB").

A thin rounded-square top plate overhangs a shallow skirt wall; at each
corner of the skirt sits a thickened block from which a square standoff leg
(rounded outer and inner vertical edges, screw hole in its foot) runs down.
The top face carries an engraved "SD-CARD USB" label and a lightning-bolt
shaped cut-out through the plate.
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0            # plate width (square)
R = 8.0              # plate corner radius
T = 2.1              # plate thickness
OVERHANG = 3.2       # plate overhang beyond the skirt wall / legs
WALL_H = 3.4         # skirt wall height below the plate
WALL_T = 2.5         # skirt wall thickness
LEG = 9.6            # leg (standoff) square size
LEG_H = 15.3         # leg height below the plate (incl. skirt height)
LEG_RO = 5.4         # leg outer corner radius (= skirt corner radius)
LEG_RI = 4.2         # leg inner corner radius
BLOCK = 11.2         # corner block inside the skirt (at wall level)
BLOCK_RI = 5.0       # inner corner radius of the corner block
HOLE_D = 3.0         # screw hole in the foot of each leg
HOLE_DEPTH = 8.0

TEXT = "SD-CARD USB"
TEXT_SIZE = 7.75     # font size
TEXT_DEPTH = 0.6     # engraving depth
TEXT_X = 9.1         # label centre
TEXT_Y = -43.9

# lightning bolt outline (through cut), plate coordinates
BOLT_PTS = [
    (-30.07, -29.16),
    (-32.26, -37.73),
    (-27.87, -36.93),
    (-30.07, -48.15),
    (-23.27, -33.17),
    (-27.41, -34.27),
    (-25.93, -29.16),
]

# ---------------- derived values ----------------
H = LEG_H + T                # overall height
A = W / 2.0 - OVERHANG       # half size of the skirt outline
ZP = H - T                   # underside of the plate
ZW = ZP - WALL_H             # bottom of the skirt wall = top of the legs
C = A - LEG / 2.0            # leg centre offset
CORNERS = [(1, 1), (-1, 1), (1, -1), (-1, -1)]


def rounded_square(size, radius, z0, height):
    """Centred square prism with rounded vertical edges."""
    return (
        cq.Workplane("XY").workplane(offset=z0)
        .sketch().rect(size, size).vertices().fillet(radius).finalize()
        .extrude(height)
    )


def corner_post(sx, sy, size, r_inner, z0, height):
    """Square post in corner (sx, sy); its inner vertical edge is rounded.
    The post is oversized outwards and later trimmed by the outline prism."""
    post = (
        cq.Workplane("XY").workplane(offset=z0)
        .center(sx * (A - size / 2.0 + 1.0), sy * (A - size / 2.0 + 1.0))
        .rect(size + 2.0, size + 2.0)
        .extrude(height)
    )
    inner_corner = (sx * (A - size), sy * (A - size), z0 + height / 2.0)
    return post.edges("|Z").edges(
        cq.selectors.NearestToPointSelector(inner_corner)
    ).fillet(r_inner)


# ---------------- top plate ----------------
plate = rounded_square(W, R, ZP, T)

# ---------------- skirt wall, corner blocks and legs ----------------
# skirt ring at wall level
keep = (
    cq.Workplane("XY").workplane(offset=ZW)
    .rect(2 * A + 2, 2 * A + 2).extrude(WALL_H)
    .cut(rounded_square(2 * (A - WALL_T), max(LEG_RO - WALL_T, 1.0), ZW, WALL_H))
)
for sx, sy in CORNERS:
    # thickened corner block inside the skirt
    keep = keep.union(corner_post(sx, sy, BLOCK, BLOCK_RI, ZW, WALL_H))
    # standoff leg hanging from the bottom of the skirt
    keep = keep.union(corner_post(sx, sy, LEG, LEG_RI, 0.0, ZW))

# one rounded outline prism trims skirt and legs -> flush rounded outer corners
outline = rounded_square(2 * A, LEG_RO, 0.0, ZP)
skirt = outline.intersect(keep)

body = plate.union(skirt)

# ---------------- screw holes in the feet ----------------
holes = (
    cq.Workplane("XY")
    .pushPoints([(sx * C, sy * C) for sx, sy in CORNERS])
    .circle(HOLE_D / 2.0)
    .extrude(HOLE_DEPTH)
)
body = body.cut(holes)

# ---------------- lightning bolt (through the plate) ----------------
bolt = (
    cq.Workplane("XY").workplane(offset=ZP)
    .polyline(BOLT_PTS).close()
    .extrude(T + 1.0)
)
body = body.cut(bolt)

# ---------------- engraved label ----------------
try:
    label = (
        cq.Workplane("XY").workplane(offset=H - TEXT_DEPTH)
        .center(TEXT_X, TEXT_Y)
        .text(TEXT, TEXT_SIZE, TEXT_DEPTH + 1.0, font="DejaVu Sans",
              halign="center", valign="center", combine=False)
    )
    engraved = body.cut(label)
    if engraved.val().isValid():
        body = engraved
except Exception:
    pass

result = body
